import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
CC = 100.0          # hub centre-to-centre distance
TILT = 11.8         # link axis tilt below +Y (deg), in the Y-Z plane
T = 10.2            # plate thickness (along X)

R1 = 18.0           # big hub (6-hole end) outer radius
R2 = 16.0           # small hub (servo end) outer radius
W = 16.0            # half width of the straight link body
RF = 30.0           # concave blend between big hub and body edges

# big hub: plain recess + 6 through holes
REC1_R = 14.0
REC1_D = 4.0
H6_PCR = 5.1
H6_R = 1.0
H6_ROT = -2.7       # angular offset of the 6-hole pattern (deg)

# servo hub: tapered recess, blind centre bore, 4 U-pockets, 8 small holes
REC2_R_TOP = 14.0   # recess radius at the face
REC2_R_BOT = 13.2   # recess radius at the floor
REC2_D = 2.8
BORE_R = 5.25
BORE_D = 5.3        # below the recess floor (blind)
POCK_PCR = 8.7      # radius of the U-pocket round ends
POCK_W = 2.5
POCK_L = 1.3        # straight run outward from the round end
POCK_D = 1.2
H8_PCR = 8.4
H8_R = 0.65
H8_D = 1.5

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived geometry ----------------
th = math.radians(TILT)
ux, uy = math.cos(th), -math.sin(th)          # link axis direction in (Y, Z)
c1 = (-CC / 2 * ux, -CC / 2 * uy)             # big hub centre (Y, Z)
c2 = (CC / 2 * ux, CC / 2 * uy)               # servo hub centre (Y, Z)
XF = T / 2                                    # front (+X) face
XB = -T / 2                                   # back face


def yz(x0):
    """Y-Z workplane (normal +X) at X = x0; local x = -Y, local y = -Z so
    circle seams fall on the -Y side (hidden from the usual views)."""
    return cq.Workplane(cq.Plane(origin=(x0, 0, 0), xDir=(0, -1, 0), normal=(1, 0, 0)))


def loc(p):
    """(Y, Z) -> local coordinates of yz()."""
    return (-p[0], -p[1])


def cyl(p, r, x0, x1):
    """Cylinder of radius r around the X-parallel axis through (Y, Z)=p, X from x0 to x1."""
    return yz(x0).center(*loc(p)).circle(r).extrude(x1 - x0)


def polar(p, rad, ang_deg):
    a = math.radians(ang_deg)
    return (p[0] + rad * math.cos(a), p[1] + rad * math.sin(a))


# ---------------- plate outline ----------------
mid = loc(((c1[0] + c2[0]) / 2, (c1[1] + c2[1]) / 2))
body = yz(XB).center(*mid).slot2D(CC + 2 * W, 2 * W, angle=-TILT).extrude(T)
plate = body.union(cyl(c1, R1, XB, XF))

# concave blends where the big hub meets the straight body edges
jedges = []
for e in plate.edges("|X").vals():
    p = e.Center()
    dy, dz = p.y - c1[0], p.z - c1[1]
    a = dy * ux + dz * uy
    n = -dy * uy + dz * ux
    if a > 0 and abs(abs(n) - W) < 0.5 and math.hypot(dy, dz) < R1 + 2:
        jedges.append(e)
if jedges:
    plate = plate.newObject(jedges).fillet(RF)

# ---------------- big hub ----------------
plate = plate.cut(cyl(c1, REC1_R, XF - REC1_D, XF + 1))
for i in range(6):
    plate = plate.cut(cyl(polar(c1, H6_PCR, H6_ROT + 60 * i), H6_R, XB - 1, XF + 1))

# ---------------- servo hub ----------------
# tapered recess (cone frustum), extended 1 mm above the face with the same taper
ext = 1.0
r_ext = REC2_R_TOP + (REC2_R_TOP - REC2_R_BOT) / REC2_D * ext
cone = cq.Solid.makeCone(
    REC2_R_BOT, r_ext, REC2_D + ext,
    pnt=cq.Vector(XF - REC2_D, c2[0], c2[1]), dir=cq.Vector(1, 0, 0),
)
cone = cone.rotate(cq.Vector(0, c2[0], c2[1]), cq.Vector(1, c2[0], c2[1]), 90)
plate = plate.cut(cq.Workplane().add(cone))

floor2 = XF - REC2_D
plate = plate.cut(cyl(c2, BORE_R, floor2 - BORE_D, floor2 + 0.5))

# 4 radial U-pockets at 45 deg: round end inward, flat end outward
for k in range(4):
    ang = 45 + 90 * k
    pc = polar(c2, POCK_PCR, ang)
    pe = polar(c2, POCK_PCR + POCK_L / 2, ang)
    rnd = cyl(pc, POCK_W / 2, floor2 - POCK_D, floor2 + 0.5)
    box = (
        yz(floor2 - POCK_D)
        .center(*loc(pe))
        .rect(POCK_L, POCK_W)
        .extrude(POCK_D + 0.5)
        .rotate((0, pe[0], pe[1]), (1, pe[0], pe[1]), ang)
    )
    plate = plate.cut(rnd.union(box))

# 8 small blind holes at 22.5 + k*45 deg
for i in range(8):
    plate = plate.cut(cyl(polar(c2, H8_PCR, 22.5 + 45 * i), H8_R, floor2 - H8_D, floor2 + 0.5))

result = plate
